import cadquery as cq
import math

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
T = 1.2                 # sheet thickness of base plate / flanges
PLATE_HALF_W = 37.3     # half width of plate (Y) at the end sections
PLATE_LEFT_X = -59.6    # left end of plate
STEP_X = 24.3           # x of the steps between end sections and middle
R_OUT = 6.5             # outer corner radius of plate (left end)
R_IN = 2.0              # corner radius at the steps

MOTOR_W = 42.3          # NEMA17 square
MOTOR_R = 6.0           # rounding of the long edges of the motor
MOTOR_L = 25.5          # length of one (pancake) motor
MOTOR_GAP = 1.0         # gap between the two back-to-back motors
MOTOR_EDGE_F = 0.4      # small fillet on the inner (seam) faces of the motors
HOLE_PITCH = 31.0       # mounting hole square
HOLE_D = 3.0
PILOT_OD = 22.2
PILOT_ID = 18.0
PILOT_H = 2.0
SHAFT_D = 5.0
FLAT_D = 0.5            # depth of the D-flat
FLAT_L = 10.0           # length of the D-flat
SHAFT_L = 12.0          # shaft protrusion beyond motor face

FLANGE_H = 9.6          # flange height above plate top
BEND_R = 0.5            # inner bend radius of flanges
FLANGE_HOLE_D = 3.4
FLANGE_HOLE_Z = 5.2      # flange hole height above plate top

SO_OD = 6.2             # standoff outer diameter
SO_ID = 3.0             # standoff bore
SO_LEFT = (-53.0, 30.8, 40.7)   # x, |y|, height
SO_RIGHT = (42.1, 25.7, 31.4)

# ---------------- derived ----------------
face_y = MOTOR_GAP / 2 + MOTOR_L          # motor outer face |y|
mid_half_w = face_y                       # middle section (up to flange inner face)
zc = T + MOTOR_W / 2                      # motor / shaft axis height

# ---------------- base plate ----------------
W = PLATE_HALF_W
left = (cq.Workplane("XY")
        .center((PLATE_LEFT_X - STEP_X) / 2, 0)
        .rect(-STEP_X - PLATE_LEFT_X, 2 * W)
        .extrude(T)
        .edges("|Z and <X").fillet(R_OUT)
        .edges("|Z and >X").fillet(R_IN))
mid = (cq.Workplane("XY")
       .rect(2 * STEP_X + 2 * R_IN, 2 * mid_half_w)
       .extrude(T))
right = (cq.Workplane("XY")
         .moveTo(STEP_X, -W)
         .lineTo(STEP_X, W)
         .threePointArc((STEP_X + W, 0), (STEP_X, -W))
         .close()
         .extrude(T))
right = right.edges("|Z").fillet(R_IN)

plate = left.union(mid).union(right)

# ---------------- bent-up flanges (L profile in YZ, extruded along X) ----
def flange(sign):
    yf = face_y
    r = BEND_R
    ro = r + T
    cy, cz = yf - r, T + r
    a45 = math.radians(45)
    prof = (cq.Workplane("YZ")
            .moveTo(yf - r - 1.0, 0)
            .lineTo(cy, 0)
            .threePointArc((cy + ro * math.sin(a45), cz - ro * math.cos(a45)),
                           (yf + T, cz))
            .lineTo(yf + T, T + FLANGE_H)
            .lineTo(yf, T + FLANGE_H)
            .lineTo(yf, cz)
            .threePointArc((cy + r * math.sin(a45), cz - r * math.cos(a45)),
                           (cy, T))
            .lineTo(yf - r - 1.0, T)
            .close()
            .extrude(MOTOR_W / 2, both=True))
    prof = prof.edges("|Y").edges(">Z").fillet(1.0)
    # two mounting holes
    holes = (cq.Workplane("XZ")
             .pushPoints([(-HOLE_PITCH / 2, T + FLANGE_HOLE_Z),
                          (HOLE_PITCH / 2, T + FLANGE_HOLE_Z)])
             .circle(FLANGE_HOLE_D / 2)
             .extrude(-(yf + 5)))
    prof = prof.cut(holes)
    if sign < 0:
        prof = prof.mirror("XZ")
    return prof

plate = plate.union(flange(1)).union(flange(-1))

# ---------------- motors ----------------
def motor(sign):
    y0 = MOTOR_GAP / 2
    body = (cq.Workplane("XZ", origin=(0, y0, zc))
            .rect(MOTOR_W, MOTOR_W)
            .extrude(-MOTOR_L)
            .edges("|Y").fillet(MOTOR_R)
            .faces("<Y").edges().fillet(MOTOR_EDGE_F)
            )
    # pilot ring on the outer face
    ring = (cq.Workplane("XZ", origin=(0, face_y, zc))
            .circle(PILOT_OD / 2).circle(PILOT_ID / 2)
            .extrude(-PILOT_H))
    shaft = (cq.Workplane("XZ", origin=(0, face_y - 1.0, zc))
             .circle(SHAFT_D / 2)
             .extrude(-(SHAFT_L + 1.0)))
    # D-flat on the underside of the shaft
    flat = (cq.Workplane("XY", origin=(0, face_y + SHAFT_L - FLAT_L / 2,
                                       zc - SHAFT_D / 2 + FLAT_D - 1.0))
            .box(SHAFT_D + 1, FLAT_L + 0.01, 2.0, centered=True))
    shaft = shaft.cut(flat)
    m = body.union(ring).union(shaft)
    if sign < 0:
        m = m.mirror("XZ")
    return m

motors = motor(1).union(motor(-1))

# through mounting holes along the motor axis
mhole_pts = [(sx * HOLE_PITCH / 2, zc + sz * HOLE_PITCH / 2)
             for sx in (-1, 1) for sz in (-1, 1)]
mholes = (cq.Workplane("XZ", origin=(0, face_y + 5, 0))
          .pushPoints(mhole_pts)
          .circle(HOLE_D / 2)
          .extrude(2 * face_y + 10))
motors = motors.cut(mholes)

# ---------------- standoffs ----------------
def standoffs(x, ay, h):
    pts = [(x, ay), (x, -ay)]
    s = (cq.Workplane("XY", origin=(0, 0, T))
         .pushPoints(pts).circle(SO_OD / 2).extrude(h))
    return s

so = standoffs(*SO_LEFT).union(standoffs(*SO_RIGHT))
bores = (cq.Workplane("XY", origin=(0, 0, -1))
         .pushPoints([(SO_LEFT[0], SO_LEFT[1]), (SO_LEFT[0], -SO_LEFT[1]),
                      (SO_RIGHT[0], SO_RIGHT[1]), (SO_RIGHT[0], -SO_RIGHT[1])])
         .circle(SO_ID / 2).extrude(60))

result = plate.union(so).union(motors).cut(bores)
